import math
import cadquery as cq

# ---------------- driving dimensions ----------------
# All sizes are first given in "drawing units" (du) and scaled to mm by S.
S = 0.2  # mm per drawing unit

# central tube (axis = Z)
TUBE_R = 31.7 * S          # outer radius
BORE_R = 29.3 * S          # bore radius
TUBE_Z0 = -102.3 * S       # bottom of tube
TUBE_Z1 = 90.5 * S         # top of tube (bore is cut up to this height)
SEAM_Z = -37.4 * S         # small step line on the tube
SEAM_STEP = 0.03           # radial size of that step (mm)
SEAM_ANGLE = 44.0          # where the periodic seam of the tube faces lies (deg)

# saddle arch (revolved about the Y axis through the origin, 180 deg over top)
ARCH_R_OUT = 103.0 * S
ARCH_R_IN = 77.4 * S
ARCH_HALF_W = 22.45 * S    # half width along Y
END_FILLET = 6.0 * S       # round on the inner edge of both arch ends

# groove in the outer face of the arch: an elliptical profile revolved about
# an axis parallel to Y that lies GROOVE_DROP below the arch axis, so the
# groove is a little deeper over the top than at the two ends
GROOVE_A = 22.33 * S       # half width of the groove (along Y)
GROOVE_B = 17.6 * S        # radial semi axis of the groove ellipse
GROOVE_END_OFF = 0.92 * S  # ellipse centre lies this far outside ARCH_R_OUT at the ends
GROOVE_DROP = 2.22 * S     # groove axis below the arch axis

# V shaped legs (4x, pin-wheel arranged, plate on one side of radial plane)
LEG_T = 13.0 * S           # plate thickness
LEG_APEX_FILLET = 12.2 * S
LEG_TIP_R = 1.0 * S
LEG_INNER_TIP_R = 3.0 * S


def P(x, z):
    return (x * S, z * S)


# leg outline in its own plane: x = radial distance, z = height
LEG_PTS = [
    P(23.0, -78.0),     # inside the bore (top inner corner)
    P(56.4, -44.7),     # apex (filleted)
    P(80.5, -133.2),    # outer prong tip, outer corner
    P(75.9, -133.9),    # outer prong tip, inner corner
    P(51.1, -80.2),     # notch vertex (sharp)
    P(27.8, -114.5),    # inner prong tip (rounded)
    P(23.0, -107.5),    # inner prong, inner edge bottom
]
LEG_RADII = [0.0, LEG_APEX_FILLET, LEG_TIP_R, LEG_TIP_R, 0.0,
             LEG_INNER_TIP_R, 0.0]


def _fillet_pts(p0, p1, p2, r):
    """tangent points and arc mid point for a fillet of radius r at p1"""
    ax, ay = p0[0] - p1[0], p0[1] - p1[1]
    bx, by = p2[0] - p1[0], p2[1] - p1[1]
    la, lb = math.hypot(ax, ay), math.hypot(bx, by)
    ax, ay, bx, by = ax / la, ay / la, bx / lb, by / lb
    t = math.acos(max(-1.0, min(1.0, ax * bx + ay * by)))
    d = r / math.tan(t / 2.0)
    t1 = (p1[0] + ax * d, p1[1] + ay * d)
    t2 = (p1[0] + bx * d, p1[1] + by * d)
    mx, my = ax + bx, ay + by
    lm = math.hypot(mx, my)
    mx, my = mx / lm, my / lm
    dc = r / math.sin(t / 2.0)
    c = (p1[0] + mx * dc, p1[1] + my * dc)
    m = (c[0] - mx * r, c[1] - my * r)
    return t1, m, t2


def rounded_outline(wp, pts, radii):
    n = len(pts)
    segs = []
    for i in range(n):
        r = radii[i]
        if r > 0:
            segs.append(_fillet_pts(pts[i - 1], pts[i], pts[(i + 1) % n], r))
        else:
            segs.append((pts[i], None, pts[i]))
    w = wp.moveTo(*segs[0][2])
    for i in range(1, n):
        t1, m, t2 = segs[i]
        w = w.lineTo(*t1)
        if m is not None:
            w = w.threePointArc(m, t2)
    w = w.lineTo(*segs[0][0])
    if segs[0][1] is not None:
        w = w.threePointArc(segs[0][1], segs[0][2])
    return w.close()


def revolve_over_top(wp):
    """revolve a profile drawn in the XY plane (x = radius, y = Y) 180 deg
    about the Y axis so that it sweeps over the top (+Z)"""
    return wp.revolve(180.0, (0, 0, 0), (0, -1, 0))


# ---------------- arch (half ring) ----------------
arch = revolve_over_top(
    cq.Workplane("XY")
    .pushPoints([((ARCH_R_OUT + ARCH_R_IN) / 2.0, 0)])
    .rect(ARCH_R_OUT - ARCH_R_IN, 2 * ARCH_HALF_W))

# round the inner edges of the two end faces
arch = arch.edges(
    cq.selectors.BoxSelector((-ARCH_R_IN - 0.5, -ARCH_HALF_W - 1, -0.5),
                             (ARCH_R_IN + 0.5, ARCH_HALF_W + 1, 0.5))
).edges("|Y").fillet(END_FILLET)

# groove tool: ellipse revolved 180 deg about the lowered axis
g_rt = math.hypot(ARCH_R_OUT + GROOVE_END_OFF, GROOVE_DROP)
groove = (revolve_over_top(
    cq.Workplane("XY")
    .pushPoints([(g_rt, 0)])
    .ellipse(GROOVE_B, GROOVE_A))
    .translate((0, 0, -GROOVE_DROP)))

# ---------------- tube ----------------
tube_low = (cq.Workplane("XY").workplane(offset=TUBE_Z0)
            .circle(TUBE_R).extrude(SEAM_Z - TUBE_Z0)
            .rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE))
tube_up = (cq.Workplane("XY").workplane(offset=SEAM_Z)
           .circle(TUBE_R - SEAM_STEP).extrude(TUBE_Z1 - SEAM_Z)
           .rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE))

body = arch.union(tube_low).union(tube_up)
# the groove also trims the top of the tube inside the arch band
body = body.cut(groove, clean=False)

# bore, cut from below up to the tube top (also opens the arch floor)
bore = (cq.Workplane("XY").workplane(offset=TUBE_Z0 - 1.0)
        .circle(BORE_R).extrude(TUBE_Z1 - TUBE_Z0 + 1.0)
        .rotate((0, 0, 0), (0, 0, 1), -45))
body = body.cut(bore)

# ---------------- legs ----------------
leg = rounded_outline(cq.Workplane("XZ"), LEG_PTS, LEG_RADII).extrude(LEG_T)
for k in range(4):
    body = body.union(leg.rotate((0, 0, 0), (0, 0, 1), 90 * k))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
